import cadquery as cq

# Round disc knob/foot: filleted rim, shallow conical faces, chamfered
# bosses top and bottom, and a locating pin underneath.

VIEW = {"azimuth": 45, "elevation": 26}

# ---- driving dimensions (mm) ----
R_OUT = 40.0        # outer radius of the disc
H_RIM = 18.5        # height of the cylindrical rim
R_FIL = 4.6         # rim edge fillet radius
R_CONE_O = 29.0     # radius where the conical face starts
R_CONE_I = 18.0     # radius where the conical face ends (central flat)
CONE_RISE_T = 2.4   # rise of top cone
CONE_RISE_B = 2.05  # rise of bottom cone
R_BOSS_B = 10.2     # boss base radius
R_BOSS_T = 8.2      # boss face radius
H_BOSS_T = 2.4      # top boss height
H_BOSS_B = 2.2      # bottom boss height
R_PIN = 2.8         # pin radius
L_PIN = 13.3        # pin length
R_BLEND = 10.0      # blend radius at the cone transitions
SEAM_ANGLE = 135.0  # angular position of the revolve seam (cosmetic)

zt = H_RIM + CONE_RISE_T
zb = -CONE_RISE_B
pts = [
    (0, zt + H_BOSS_T),
    (R_BOSS_T, zt + H_BOSS_T),
    (R_BOSS_B, zt),
    (R_CONE_I, zt),
    (R_CONE_O, H_RIM),
    (R_OUT, H_RIM),
    (R_OUT, 0),
    (R_CONE_O, 0),
    (R_CONE_I, zb),
    (R_BOSS_B, zb),
    (R_BOSS_T, zb - H_BOSS_B),
    (R_PIN, zb - H_BOSS_B),
    (R_PIN, zb - H_BOSS_B - L_PIN),
    (0, zb - H_BOSS_B - L_PIN),
]

body = (cq.Workplane("XZ").polyline(pts).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))


class _RadiusSel(cq.Selector):
    def __init__(self, r, tol=1e-3):
        self.r = r
        self.tol = tol

    def filter(self, objs):
        return [o for o in objs
                if o.geomType() == "CIRCLE" and abs(o.radius() - self.r) < self.tol]


# round the two outer rim edges
body = body.edges(_RadiusSel(R_OUT)).fillet(R_FIL)
# blend the shallow conical faces into the flats
body = body.edges(_RadiusSel(R_CONE_O)).fillet(R_BLEND)
body = body.edges(_RadiusSel(R_CONE_I)).fillet(R_BLEND)

# turn the revolve seam to the rear of the main view (purely cosmetic)
result = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
